import math
import cadquery as cq

# ---------------------------------------------------------------
# Two-piece snap-fit enclosure: base tray (+Y) and lid (-Y),
# both shown open side up, side by side.
# ---------------------------------------------------------------

L = 118.0          # length of both halves (X)
W = 40.0           # width of both halves (Y)
GAP = 14.4         # gap between the two bodies (Y)
T = 2.6            # wall thickness
TF = 2.0           # floor thickness
R_V = 2.0          # outer vertical corner radius
R_TOP = 0.4        # small round on the outer top edges

# base tray
H_T = 11.0         # tray height
XP = 28.0          # tray partition centre (X)
TP = 2.8           # partition thickness
END_DROP_T = 5.0   # lowered -X end wall of tray
CORNER_LEN = 8.0   # raised corner length on lowered end walls
HOLE_D = 6.0
HOLE_X = 44.9
WIN_Z0, WIN_Z1 = 4.6, 8.4   # snap windows in tray side walls
WIN_DEPTH = 1.3
SNAP_X = [(12.8, 42.5), (85.4, 114.6)]   # measured from -X end
HOOK_X = [(12.0, 41.9), (84.6, 114.3)]   # lid hook ribs, from -X end
NOTCH_D = 0.9      # inner locating notch depth
NOTCH_H = 2.2      # inner locating notch height

# lid
H_L = 13.0         # lid height
END_DROP_L = 4.8   # lowered -X end wall of lid
NOTCH_W = 10.5     # U notch in +X end wall
NOTCH_BOT = 5.0    # z of notch bottom
FLAP_T = 2.6       # snap flap thickness
FLAP_Z = (3.85, 9.6, 17.0, 20.5)   # flap profile heights
FLAP_BLEND = 8.0   # blend radius at both ends of the lower flap chamfer
FLAP_X0 = 11.4     # from -X end
FLAP_X1 = 2.5      # from +X end
HOOK_Z = (15.6, 16.6, 18.4, 19.4)
HOOK_D = 1.4
POST_TOP = H_L + 1.6
POST_IN = 0.85     # lid posts are partly sunk into the side wall
SLOT_N = 9
SLOT_PITCH = 6.1
SLOT_LEN = 30.8
SLOT_W = 1.3
SLOT_ANG = -62.0
SLOT_CX = -11.2
LOGO_D = 30.0
LOGO_X = L / 2 - 19.6

YT = GAP / 2 + W / 2      # tray centre Y
YL = -(GAP / 2 + W / 2)   # lid centre Y
X0 = -L / 2


def box(x0, x1, y0, y1, z0, z1):
    return (cq.Workplane("XY")
            .box(x1 - x0, y1 - y0, z1 - z0, centered=False)
            .translate((x0, y0, z0)))


def shell_body(yc, h):
    outer = (cq.Workplane("XY").rect(L, W).extrude(h)
             .edges("|Z").fillet(R_V)
             .faces(">Z").edges().fillet(R_TOP)
             .translate((0, yc, 0)))
    inner = box(-L / 2 + T, L / 2 - T, yc - W / 2 + T, yc + W / 2 - T, TF, h + 1)
    return outer.cut(inner)


# ------------------------------- tray --------------------------------
tray = shell_body(YT, H_T)
# partition wall
tray = tray.union(box(XP - TP / 2, XP + TP / 2, YT - W / 2 + 1, YT + W / 2 - 1, 0, H_T))
# lowered middle of -X end wall
tray = tray.cut(box(X0 - 1, X0 + T + 0.01, YT - W / 2 + CORNER_LEN,
                    YT + W / 2 - CORNER_LEN, H_T - END_DROP_T, H_T + 1))
# mounting holes
for hx in (-HOLE_X, HOLE_X):
    tray = tray.cut(cq.Workplane("XY").circle(HOLE_D / 2).extrude(H_T)
                    .translate((hx, YT, -1)))
    tray = tray.cut(cq.Workplane("XY").circle(HOLE_D / 2 + 0.8)
                    .workplane(offset=0.8).circle(HOLE_D / 2).loft()
                    .translate((hx, YT, -0.001)))


# wedge posts with sloped inner face
def wedge_post(xa, xb, y_wall, sgn, top, depth=5.0, flat=2.2):
    # sgn = +1 -> post grows toward +Y from wall
    pts = [(0, TF - 0.01), (0, top), (flat, top), (depth, TF - 0.01)]
    prof = [(y_wall + sgn * s, z) for s, z in pts]
    return (cq.Workplane("YZ").polyline(prof).close()
            .extrude(xb - xa).translate((xa, 0, 0)))


POST_T_TOP = 6.6
yi_p = YT + W / 2 - T     # inner +Y wall face
yi_m = YT - W / 2 + T     # inner -Y wall face
tray_posts = [
    # (xa, xb, side)  side +1: against +Y wall, -1: against -Y wall
    (X0 + T, X0 + 9.0, +1),
    (X0 + T, X0 + 9.0, -1),
    (XP - TP / 2 - 5.8, XP - TP / 2 - 1.0, +1),
    (XP - TP / 2 - 4.8, XP - TP / 2, -1),
    (L / 2 - T - 6.3, L / 2 - T - 1.5, +1),
    (L / 2 - T - 4.8, L / 2 - T, -1),
]
for (xa, xb, side) in tray_posts:
    if side > 0:
        tray = tray.union(wedge_post(xa, xb, yi_p, -1, POST_T_TOP))
    else:
        tray = tray.union(wedge_post(xa, xb, yi_m, +1, POST_T_TOP))

# small locating notches at the top of the inner side walls above the posts
# (they receive the lid posts when the lid is closed)
tray_notches = [
    (X0 + T + 0.6, X0 + 8.4, +1),
    (X0 + T + 0.6, X0 + 8.4, -1),
    (X0 + 81.0, X0 + 85.3, -1),
    (L / 2 - 7.6, L / 2 - T - 0.6, -1),
]
for (xa, xb, sg) in tray_notches:
    if sg > 0:
        tray = tray.cut(box(xa, xb, yi_p - 0.1, yi_p + NOTCH_D, H_T - NOTCH_H, H_T + 1))
    else:
        tray = tray.cut(box(xa, xb, yi_m - NOTCH_D, yi_m + 0.1, H_T - NOTCH_H, H_T + 1))

# snap windows in the outside of the long walls
for (a, b) in SNAP_X:
    for (y0, y1) in [(YT + W / 2 - WIN_DEPTH, YT + W / 2 + 1),
                     (YT - W / 2 - 1, YT - W / 2 + WIN_DEPTH)]:
        tray = tray.cut(box(X0 + a, X0 + b, y0, y1, WIN_Z0, WIN_Z1))

# ------------------------------- lid ---------------------------------
lid = shell_body(YL, H_L)
# lowered middle of -X end wall
lid = lid.cut(box(X0 - 1, X0 + T + 0.01, YL - W / 2 + CORNER_LEN,
                  YL + W / 2 - CORNER_LEN, H_L - END_DROP_L, H_L + 1))
# U notch in +X end wall
r_n = NOTCH_W / 2
notch = (cq.Workplane("YZ").center(YL, NOTCH_BOT + r_n)
         .circle(r_n).extrude(T + 2)
         .union(cq.Workplane("YZ").center(YL, (NOTCH_BOT + r_n + H_L + 2) / 2)
                .rect(NOTCH_W, H_L + 2 - NOTCH_BOT - r_n).extrude(T + 2))
         .translate((L / 2 - T - 1, 0, 0)))
lid = lid.cut(notch)


def post(xa, xb, y_wall, sgn, d_top, d_bot, top, ch=1.0):
    # tapered locating post standing on the lid floor against a side wall
    prof = [(y_wall + sgn * POST_IN, TF - 0.01), (y_wall - sgn * d_bot, TF - 0.01),
            (y_wall - sgn * d_top, top), (y_wall + sgn * POST_IN, top)]
    p = (cq.Workplane("YZ").polyline(prof).close()
         .extrude(xb - xa).translate((xa, 0, 0)))
    return p.faces(">Z").edges().chamfer(ch)


yli_p = YL + W / 2 - T
yli_m = YL - W / 2 + T
lid_posts = [
    # (xa, xb, wall y, sign, depth top, depth bottom)
    (X0 + T - 0.3, X0 + 8.2, yli_p, +1, 3.5, 5.2),
    (X0 + T - 0.3, X0 + 8.2, yli_m, -1, 3.5, 5.2),
    (X0 + 81.1, X0 + 85.2, yli_p, +1, 3.5, 6.5),
    (X0 + 85.6, X0 + 88.4, yli_m, -1, 3.5, 4.8),
    (L / 2 - 7.5, L / 2 - T + 0.3, yli_p, +1, 3.5, 4.8),
]
for (xa, xb, yw_, sg, dt, db) in lid_posts:
    lid = lid.union(post(xa, xb, yw_, sg, dt, db, POST_TOP))

# vent slots through the floor
for i in range(SLOT_N):
    cx = SLOT_CX + (i - (SLOT_N - 1) / 2) * SLOT_PITCH
    s = (cq.Workplane("XY").slot2D(SLOT_LEN, SLOT_W, SLOT_ANG).extrude(TF + 2)
         .translate((cx, YL, -1)))
    lid = lid.cut(s)


# snap flaps on both long sides
def flap(sgn):
    # sgn=-1 -> -Y side, sgn=+1 -> +Y side
    yw = YL + sgn * W / 2
    z0, z1, z2, z3 = FLAP_Z
    xa = X0 + FLAP_X0
    xb = L / 2 - FLAP_X1
    # profile: lower chamfer blended tangentially into the wall and into the
    # vertical outer face (arc - line - arc), then the top chamfer
    al = math.atan(FLAP_T / (z1 - z0))
    rb = FLAP_BLEND
    tau = rb * math.tan(al / 2)
    zc1 = z0 - tau
    zc2 = z1 + tau

    def p1(phi):
        return (yw + sgn * rb * (1 - math.cos(phi)), zc1 + rb * math.sin(phi))

    def p2(psi):
        return (yw + sgn * (FLAP_T - rb * (1 - math.cos(psi))),
                zc2 - rb * math.sin(psi))

    sec = (cq.Workplane("YZ")
           .moveTo(yw - sgn * 1.0, zc1)
           .lineTo(yw, zc1)
           .threePointArc(p1(al / 2), p1(al))
           .lineTo(*p2(al))
           .threePointArc(p2(al / 2), p2(0.0))
           .lineTo(yw + sgn * FLAP_T, z2)
           .lineTo(yw, z3)
           .lineTo(yw, H_L)
           .lineTo(yw - sgn * 0.6, H_L)
           .lineTo(yw - sgn * 0.6, H_L - 0.5)
           .lineTo(yw - sgn * 1.0, H_L - 0.5)
           .close()
           .extrude(xb - xa).translate((xa, 0, 0)))
    foot = (cq.Workplane("XY")
            .polyline([(xa, yw - sgn * 1.2), (xb, yw - sgn * 1.2),
                       (xb, yw), (xb - FLAP_T, yw + sgn * FLAP_T),
                       (xa + FLAP_T, yw + sgn * FLAP_T), (xa, yw)]).close()
            .extrude(z3 + 1).translate((0, 0, -0.5)))
    f = sec.intersect(foot)
    # hook ribs on the inner face, above the wall top
    h0, h1, h2, h3 = HOOK_Z
    hp = [(yw, h0), (yw - sgn * HOOK_D, h1), (yw - sgn * HOOK_D, h2), (yw, h3)]
    for (a, b) in HOOK_X:
        ha = X0 + a
        hb = X0 + b
        hk = (cq.Workplane("YZ").polyline(hp).close()
              .extrude(hb - ha).translate((ha, 0, 0)))
        hfoot = (cq.Workplane("XY")
                 .polyline([(ha, yw + sgn * 0.01), (hb, yw + sgn * 0.01),
                            (hb - HOOK_D, yw - sgn * HOOK_D),
                            (ha + HOOK_D, yw - sgn * HOOK_D)]).close()
                 .extrude(30).translate((0, 0, -1)))
        f = f.union(hk.intersect(hfoot))
    return f


lid = lid.union(flap(-1)).union(flap(+1))

# logo (circle with stylised "N" bolt): engraved underneath and inside
LOGO_R = LOGO_D / 2
LOGO_DEPTH = 0.35


def logo_cutter(z0, depth):
    # shallow round recess leaving the two bolt shapes standing
    rin = LOGO_R * 0.9
    disc = cq.Workplane("XY").circle(LOGO_R).extrude(depth)
    inner = cq.Workplane("XY").circle(rin).extrude(depth)
    sa = [(-0.60, 0.95), (-0.60, -0.30), (0.50, 0.72), (0.50, 0.95)]
    sb = [(0.69, 0.62), (0.69, -0.95), (-0.60, -0.95), (-0.56, -0.76),
          (0.60, 0.28)]
    cut = disc
    for pts in (sa, sb):
        poly = (cq.Workplane("XY")
                .polyline([(u * LOGO_R, v * LOGO_R) for u, v in pts]).close()
                .extrude(depth))
        cut = cut.cut(poly.intersect(inner))
    return cut.translate((LOGO_X, YL, z0))


lid = lid.cut(logo_cutter(-0.01, LOGO_DEPTH + 0.01))
lid = lid.cut(logo_cutter(TF - LOGO_DEPTH, LOGO_DEPTH + 0.01))

result = tray.union(lid)
